import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 20.0             # disk outer radius
T_TOTAL = 1.9        # overall thickness (back face -> rim top / tab face)
RECESS = 0.6         # depth of the recessed front field below the rim top
RIM_W = 1.85         # radial width of the raised rim
RIM_CHAMFER = 0.5    # bevel of the rim's inner edge
EDGE_CHAMFER = 0.3   # soft bevel of the outer perimeter edges

# hanging tab (circular-arc top, slanted sides)
TAB_ARC_R = 16.3     # radius of the tab's top arc
TAB_ARC_CZ = 9.75    # Z of the top-arc centre
TAB_HALF_W = 11.7    # half width at the tab's top corners
TAB_SIDE_DX = 2.42   # inward run of the slanted sides ...
TAB_SIDE_DZ = -3.45  # ... per this drop
TAB_CORNER_R = 0.5   # in-plane rounding of the tab's top corners

# cross shaped hole in the tab
CROSS_Z = 22.05
CROSS_L = 4.4
CROSS_W = 1.6
CROSS_FILLET = 0.15

# text
TEXT_H = 0.4         # raised text height on the front field
BACK_TEXT_D = 0.1    # engraving depth of the mirrored text on the back
FONT = "DejaVu Sans"
TEXT_SX = 0.86       # horizontal condensing of the glyphs
# (line, font size, baseline Z, [(char, centre X), ...])
TEXT_LINES = [
    (8.55, 4.6, [("N", -9.08), ("u", -3.37), ("r", 1.61), ("s", 5.24), ("e", 9.89)]),
    (9.2, -3.66, [("2", -5.5), ("0", -0.03), ("0", 5.39)]),
    (8.7, -11.4, [("B", -8.7), ("A", -3.35), ("C", 2.82), ("K", 8.65)]),
]

# shallow groove in the rim top on the left edge, ending in ratchet teeth
GROOVE_A0 = 158.0      # deg, start of groove (from +X, CCW seen from front)
GROOVE_R_IN = 18.5     # inner radius of the plain groove part
GROOVE_R_OUT = 19.6    # outer radius (leaves a thin outer lip)
TOOTH_A0 = 188.4       # deg, first tooth
TOOTH_PITCH = 4.84     # deg
TOOTH_RAMP = 3.9       # deg of the ramp part of each tooth
TOOTH_R_PEAK = 19.4
TOOTH_R_VALLEY = 18.5
N_TEETH = 6
GROOVE_DEPTH = 0.2

# ---------------- body ----------------
XZ = cq.Plane.named("XZ")   # normal -Y : extrusion goes toward the front

disk = cq.Workplane(XZ).circle(R).extrude(T_TOTAL)

# tab outline (the part inside the disk just overlaps it)
tl = (-TAB_HALF_W, TAB_ARC_CZ + math.sqrt(TAB_ARC_R**2 - TAB_HALF_W**2))
tr = (TAB_HALF_W, tl[1])
k = 2.2
bl = (tl[0] + k * TAB_SIDE_DX, tl[1] + k * TAB_SIDE_DZ)
br = (-bl[0], bl[1])
tab = (
    cq.Workplane(XZ)
    .moveTo(*bl)
    .lineTo(*tl)
    .threePointArc((0, TAB_ARC_CZ + TAB_ARC_R), tr)
    .lineTo(*br)
    .close()
    .extrude(T_TOTAL)
)
body = disk.union(tab)
corner_edges = [
    e for e in body.edges("|Y").vals()
    if min(abs(e.Center().x - c[0]) + abs(e.Center().z - c[1]) for c in (tl, tr)) < 1e-3
]
body = body.newObject(corner_edges).fillet(TAB_CORNER_R)

# recessed front field
recess = (
    cq.Workplane(XZ)
    .workplane(offset=T_TOTAL - RECESS)
    .circle(R - RIM_W)
    .extrude(RECESS + 1.0)
)
body = body.cut(recess)


# bevel the inner rim edge, then soften the outer perimeter (front and back)
def _is_rim_circle(e):
    return e.geomType() == "CIRCLE" and abs(e.radius() - (R - RIM_W)) < 1e-3


inner = [e for e in body.faces("<Y").edges().vals() if _is_rim_circle(e)]
body = body.newObject(inner).chamfer(RIM_CHAMFER)
outer = [e for e in body.faces("<Y").edges().vals() if not _is_rim_circle(e)]
body = body.newObject(outer).chamfer(EDGE_CHAMFER)
body = body.faces(">Y").edges().chamfer(EDGE_CHAMFER)


# ---------------- rim groove with ratchet teeth ----------------
def pol(r, a):
    return (r * math.cos(math.radians(a)), r * math.sin(math.radians(a)))


teeth = []
for i in range(N_TEETH):
    a = TOOTH_A0 + i * TOOTH_PITCH
    teeth.append(pol(TOOTH_R_PEAK, a))
    teeth.append(pol(TOOTH_R_VALLEY, a + TOOTH_RAMP))
a_end = TOOTH_A0 + (N_TEETH - 1) * TOOTH_PITCH + TOOTH_RAMP + 0.3
groove = (
    cq.Workplane(XZ)
    .workplane(offset=T_TOTAL - GROOVE_DEPTH)
    .moveTo(*pol(GROOVE_R_OUT, GROOVE_A0))
    .lineTo(*pol(GROOVE_R_IN, GROOVE_A0))
    .threePointArc(pol(GROOVE_R_IN, 0.5 * (GROOVE_A0 + TOOTH_A0)),
                   pol(GROOVE_R_IN, TOOTH_A0))
    .polyline([pol(GROOVE_R_IN, TOOTH_A0)] + teeth + [pol(GROOVE_R_OUT, a_end)])
    .threePointArc(pol(GROOVE_R_OUT, 0.5 * (GROOVE_A0 + a_end)),
                   pol(GROOVE_R_OUT, GROOVE_A0))
    .close()
    .extrude(1.0)
)
body = body.cut(groove)

# ---------------- cross hole ----------------
def _bar(w, h):
    return (
        cq.Workplane(XZ)
        .workplane(offset=-1.0)
        .center(0, CROSS_Z)
        .rect(w, h)
        .extrude(T_TOTAL + 2.0)
    )


cross = _bar(CROSS_L, CROSS_W).union(_bar(CROSS_W, CROSS_L)).edges("|Y").fillet(CROSS_FILLET)
body = body.cut(cross)


# ---------------- text ----------------
def glyph_solids(ch, fs, cx, zb, y_base, h):
    """Glyph outline, condensed in X, centred at cx on baseline zb, extruded
    from plane Y=y_base toward -Y by h."""
    flat = cq.Compound.makeText(ch, fs, 0, font=FONT, kind="bold",
                                halign="left", valign="bottom")
    bb = flat.BoundingBox()
    xc = 0.5 * (bb.xmin + bb.xmax)
    m = cq.Matrix([[TEXT_SX, 0, 0, cx - TEXT_SX * xc],
                   [0, 1, 0, zb],
                   [0, 0, 1, 0],
                   [0, 0, 0, 1]])
    pl = cq.Plane(origin=(0, y_base, 0), xDir=(1, 0, 0), normal=(0, -1, 0))
    out = []
    for f in flat.Faces():
        ow = f.outerWire().transformGeometry(m)
        iws = [w.transformGeometry(m) for w in f.innerWires()]
        s = cq.Solid.extrudeLinear(ow, iws, (0, 0, h))
        out.append(s.transformShape(pl.rG))
    return out


def text_body(y_base, h):
    solids = []
    for fs, zb, chars in TEXT_LINES:
        for ch, cx in chars:
            solids.extend(glyph_solids(ch, fs, cx, zb, y_base, h))
    wp = cq.Workplane(XZ).newObject([solids[0]])
    for s in solids[1:]:
        wp = wp.union(cq.Workplane(XZ).newObject([s]))
    return wp


front_text = text_body(-(T_TOTAL - RECESS) + 0.02, TEXT_H + 0.02)
body = body.union(front_text)
back_text = text_body(0.5, 0.5 + BACK_TEXT_D)
body = body.cut(back_text)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
